import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Funnel / cone adapter with front flange, raised sealing bead around the
# mouth, cross rib in the mouth, two side lugs and a tapered hose spigot.
# Axis of revolution = global Y.  The wide mouth faces -Y (front), the spigot
# points to +Y.  Flange front face lies in the plane y = 0.
# ---------------------------------------------------------------------------

# --- flange ---------------------------------------------------------------
R_FL = 50.0        # flange outer radius
T_FL = 6.35        # flange thickness (front face y=0, back face y=T_FL)
CH_FL = 1.05       # chamfer on flange front outer edge

# --- raised sealing bead and mouth ----------------------------------------
R_RING = 40.7      # outer radius of raised bead at its base (flange face)
R_RING_F = 40.2    # outer radius of raised bead at its front (draft)
H_RING = 4.1       # bead protrusion in front of the flange face
R_STEP = 35.9      # inner wall of the bead (step down to the mouth land)
Y_LAND = -0.2      # axial position of the flat land inside the bead
FIL_BEAD_O = 1.0   # round on bead outer front edge
FIL_BEAD_I = 0.6   # round on bead inner front edge
FIL_STEP = 0.4     # cove between bead inner wall and land
R_OPEN = 27.9      # mouth radius where the funnel bore starts
CH_OPEN = 0.5      # small chamfer on the mouth edge
Y_OPEN = Y_LAND + CH_OPEN  # axial position of mouth radius R_OPEN

# --- cone / spigot ------------------------------------------------------
R_KINK = 45.3      # end of steep transition cone behind the flange
Y_KINK = 10.9      # axial position of that transition
Y_TUBE = 49.7      # axial position of cone -> spigot junction
R_TUBE0 = 17.15    # spigot outer radius at junction
R_TUBE1 = 15.9     # spigot outer radius at free end (tapered spigot)
Y_END = 85.15      # free end of spigot
CH_TUBE = 1.2      # outer chamfer at spigot end
R_BORE0 = 12.4     # spigot bore radius at the funnel end
R_BORE1 = 12.4     # spigot bore radius at the free end (draft)

# --- cross rib in mouth -------------------------------------------------
RIB_T = 4.0        # rib thickness (Z)
RIB_Y0 = 0.0       # rib front edge (axial)
RIB_NOTCH_Y = 4.8  # V-notch apex distance behind rib front edge
RIB_NOTCH_A = 41.0 # half angle of V notch arms (deg from axis)

# --- side lugs ----------------------------------------------------------
LUG_T = 2.5        # lug thickness (Z)
LUG_R = 53.2       # lug tip radius
LUG_TIP_D = 2.4    # axial depth of lug at tip
LUG_FIL = 0.3      # round on the lug tip edges


def fillet_corner(a, b, c, r):
    """Tangent points and arc mid point of a fillet of radius r at corner b."""
    u1 = (a[0] - b[0], a[1] - b[1])
    u2 = (c[0] - b[0], c[1] - b[1])
    l1 = math.hypot(*u1)
    l2 = math.hypot(*u2)
    u1 = (u1[0] / l1, u1[1] / l1)
    u2 = (u2[0] / l2, u2[1] / l2)
    cosang = max(-1.0, min(1.0, u1[0] * u2[0] + u1[1] * u2[1]))
    th = math.acos(cosang)
    d = r / math.tan(th / 2.0)
    t1 = (b[0] + u1[0] * d, b[1] + u1[1] * d)
    t2 = (b[0] + u2[0] * d, b[1] + u2[1] * d)
    w = (u1[0] + u2[0], u1[1] + u2[1])
    lw = math.hypot(*w)
    w = (w[0] / lw, w[1] / lw)
    oc = r / math.sin(th / 2.0)
    o = (b[0] + w[0] * oc, b[1] + w[1] * oc)
    m = (o[0] - w[0] * r, o[1] - w[1] * r)
    return t1, t2, m


def build_profile(nodes):
    """nodes: list of (point, fillet_radius).  Returns a closed Workplane wire
    in the XY plane (x = radius, y = axial) with tangent-arc fillets."""
    n = len(nodes)
    pts = [p for p, _ in nodes]
    corners = []
    for i, (p, r) in enumerate(nodes):
        if r > 0:
            corners.append(fillet_corner(pts[i - 1], p, pts[(i + 1) % n], r))
        else:
            corners.append((p, p, None))
    wp = cq.Workplane("XY").moveTo(*corners[0][1])
    for k in range(1, n + 1):
        t1, t2, m = corners[k % n]
        wp = wp.lineTo(*t1)
        if m is not None:
            wp = wp.threePointArc(m, t2)
    return wp.close()


def revolve_y(wp):
    return wp.revolve(360, (0, 0, 0), (0, 1, 0))


# ---------------------------------------------------------------------------
# Revolved main body (half cross-section in the r / axial plane)
# ---------------------------------------------------------------------------
nodes = [
    ((R_OPEN, Y_OPEN), 0),                         # start of funnel bore
    ((R_OPEN + CH_OPEN, Y_LAND), 0),               # mouth edge chamfer
    ((R_STEP, Y_LAND), FIL_STEP),                  # land -> bead inner wall
    ((R_STEP, -H_RING), FIL_BEAD_I),               # bead inner front edge
    ((R_RING_F, -H_RING), FIL_BEAD_O),             # bead outer front edge
    ((R_RING, 0.0), 0.5),                          # bead base / flange face
    ((R_FL - CH_FL, 0.0), 0),                      # flange face
    ((R_FL, CH_FL), 0),                            # flange chamfer
    ((R_FL, T_FL), 0),                             # flange back corner
    ((R_KINK, Y_KINK), 0),                         # steep transition cone
    ((R_TUBE0, Y_TUBE), 0),                        # cone -> spigot
    ((R_TUBE1, Y_END - CH_TUBE), 0),               # spigot end chamfer
    ((R_TUBE1 - CH_TUBE, Y_END), 0),               # spigot end face
    ((R_BORE1, Y_END), 0.3),                       # bore edge
    ((R_BORE0, Y_TUBE), 0),                        # bore -> funnel cone
]
body = revolve_y(build_profile(nodes))

# ---------------------------------------------------------------------------
# Cross rib in the mouth: flat plate in the XY plane bounded by the funnel
# wall, with a V-notch cut into its back edge.
# ---------------------------------------------------------------------------
cavity = revolve_y(
    cq.Workplane("XY")
    .polyline([(0, Y_LAND), (R_OPEN + CH_OPEN, Y_LAND), (R_OPEN, Y_OPEN), (R_BORE0, Y_TUBE), (0, Y_TUBE)])
    .close()
)
rib = cq.Workplane("XY").box(2 * R_OPEN + 4, 45.0, RIB_T, centered=(True, False, True)).translate((0, RIB_Y0, 0))
ya = RIB_Y0 + RIB_NOTCH_Y
L = 80.0
ta = math.tan(math.radians(RIB_NOTCH_A))
notch = (
    cq.Workplane("XY")
    .polyline([(0, ya), (-L * ta, ya + L), (L * ta, ya + L)])
    .close()
    .extrude(RIB_T + 2)
    .translate((0, 0, -(RIB_T + 2) / 2))
)
rib = rib.cut(notch).intersect(cavity)

# ---------------------------------------------------------------------------
# Side lugs on +/-X: wedges on the flange rim, front face just behind the
# flange chamfer, sloping back face running into the flange back edge.
# ---------------------------------------------------------------------------
lug_pts = [
    (R_FL - 1.0, CH_FL),
    (LUG_R, CH_FL),
    (LUG_R, CH_FL + LUG_TIP_D),
    (R_FL, T_FL),
    (R_FL - 1.0, T_FL),
]
lug_r = (
    cq.Workplane("XY")
    .polyline(lug_pts)
    .close()
    .extrude(LUG_T)
    .translate((0, 0, -LUG_T / 2))
    .edges("|Y")
    .edges(">X")
    .fillet(LUG_FIL)
)
lug_l = lug_r.mirror("YZ")

result = body.union(rib).union(lug_r).union(lug_l)

VIEW = {"azimuth": 45, "elevation": 26}
